import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # tray length (X)
W = 93.6           # tray depth (Y)
H = 22.5           # tray height (Z)
GAP = 18.2         # gap between the two trays (Y)
T_WALL = 1.6       # wall thickness
T_FLOOR = 3.8      # floor thickness

# screw bosses / grooves
BOSS_R = 1.55
BOSS_INSET = 1.6           # boss axis distance from the outer wall face
BOSS_HOLE_R = 0.6
BOSS_END = 14.4            # boss distance from tray end
GROOVE_W = 2.2            # outer vertical groove width
GROOVE_D = 0.8            # groove depth into the wall
GROOVE_TOP_GAP = 1.3      # groove stops this far below the rim
FRONT_MID_SHIFT = -5.3     # middle boss shift on the lid's outer (-Y) wall
HANG_BOSS_LEN = 4.9        # hanging boss length (base tray)

# connector cut-outs on base tray long walls
CONN_X = 66.2
CONN_W = 16.4
CONN_H = 8.5
CONN_ZC_FROM_TOP = 13.9
CONN_HOLE_DX = 10.4
CONN_HOLE_D = 1.25
SLOT_L = 12.8
SLOT_H = 2.8
SLOT_Z_FROM_TOP = 6.4

# floor holes of the base tray
FLOOR_HOLES_X = (-28.1, 21.7)
FLOOR_HOLES_Y = 20.5
FLOOR_HOLE_D = 1.4
FLOOR_SLOT_X = 39.3
FLOOR_SLOT_W = 2.6
FLOOR_SLOT_L = 5.4

# end-wall holes
LID_END_HOLE_D = 6.0
LID_END_HOLE_Y = 2.9
LID_END_HOLE_Z_FROM_TOP = 4.75
BASE_END_HOLE_D = 2.6
BASE_END_HOLE_Y = -9.7
BASE_END_HOLE_Z_FROM_TOP = 7.8


def tray_shell():
    outer = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))
    cavity = (cq.Workplane("XY").workplane(offset=T_FLOOR)
              .rect(L - 2 * T_WALL, W - 2 * T_WALL).extrude(H))
    return outer.cut(cavity)


def lid_tray():
    """Front tray: plain floor, grooved long walls with full-height bosses."""
    body = tray_shell()
    xs_back = [-L / 2 + BOSS_END, 0.0, L / 2 - BOSS_END]
    xs_front = [-L / 2 + BOSS_END, FRONT_MID_SHIFT, L / 2 - BOSS_END]
    for side, xs in ((1, xs_back), (-1, xs_front)):
        y_in = side * (W / 2 - BOSS_INSET)
        y_out = side * (W / 2)
        for x in xs:
            boss = (cq.Workplane("XY").workplane(offset=T_FLOOR - 0.01)
                    .center(x, y_in).circle(BOSS_R).extrude(H - T_FLOOR + 0.01))
            body = body.union(boss)
            gh = H - GROOVE_TOP_GAP + 1.0
            groove = (cq.Workplane("XY")
                      .box(GROOVE_W, 2 * GROOVE_D, gh)
                      .translate((x, y_out, gh / 2 - 1.0)))
            body = body.cut(groove)
            hole = (cq.Workplane("XY").workplane(offset=T_FLOOR + 1.0)
                    .center(x, y_in).circle(BOSS_HOLE_R).extrude(H))
            body = body.cut(hole)
    # round hole in the -X end wall
    end_hole = (cq.Workplane("YZ").workplane(offset=-L / 2 - 1)
                .center(LID_END_HOLE_Y, H - LID_END_HOLE_Z_FROM_TOP)
                .circle(LID_END_HOLE_D / 2).extrude(T_WALL + 2))
    body = body.cut(end_hole)
    return body


def base_tray():
    """Back tray: floor holes, connector windows, hanging screw bosses."""
    body = tray_shell()
    xs = [-L / 2 + BOSS_END, 0.0, L / 2 - BOSS_END]
    for side in (1, -1):
        y_in = side * (W / 2 - BOSS_INSET)
        for x in xs:
            boss = (cq.Workplane("XY").workplane(offset=H - HANG_BOSS_LEN)
                    .center(x, y_in).circle(BOSS_R).extrude(HANG_BOSS_LEN))
            body = body.union(boss)
            hole = (cq.Workplane("XY").workplane(offset=H - HANG_BOSS_LEN + 1.0)
                    .center(x, y_in).circle(BOSS_HOLE_R).extrude(HANG_BOSS_LEN))
            body = body.cut(hole)
        # connector windows + mounting holes + slot above
        for cx in (-CONN_X, CONN_X):
            zc = H - CONN_ZC_FROM_TOP
            cutter = (cq.Workplane("XY").box(CONN_W, T_WALL * 3, CONN_H)
                      .translate((cx, side * (W / 2 - T_WALL / 2), zc)))
            body = body.cut(cutter)
            for dx in (-CONN_HOLE_DX, CONN_HOLE_DX):
                h = (cq.Workplane("XZ").center(cx + dx, zc)
                     .circle(CONN_HOLE_D / 2).extrude(T_WALL * 1.5, both=True)
                     .translate((0, side * (W / 2 - T_WALL / 2), 0)))
                body = body.cut(h)
            s = (cq.Workplane("XZ").center(cx, H - SLOT_Z_FROM_TOP)
                 .ellipse(SLOT_L / 2, SLOT_H / 2).extrude(T_WALL * 1.5, both=True)
                 .translate((0, side * (W / 2 - T_WALL / 2), 0)))
            body = body.cut(s)
    # floor holes and slot
    pts = [(x, y) for x in FLOOR_HOLES_X for y in (-FLOOR_HOLES_Y, FLOOR_HOLES_Y)]
    fh = (cq.Workplane("XY").workplane(offset=-1).pushPoints(pts)
          .circle(FLOOR_HOLE_D / 2).extrude(T_FLOOR + 2))
    body = body.cut(fh)
    fs = (cq.Workplane("XY").workplane(offset=-1).center(FLOOR_SLOT_X, 0)
          .rect(FLOOR_SLOT_W, FLOOR_SLOT_L).extrude(T_FLOOR + 2))
    body = body.cut(fs)
    # small hole in the -X end wall
    end_hole = (cq.Workplane("YZ").workplane(offset=-L / 2 - 1)
                .center(BASE_END_HOLE_Y, H - BASE_END_HOLE_Z_FROM_TOP)
                .circle(BASE_END_HOLE_D / 2).extrude(T_WALL + 2))
    body = body.cut(end_hole)
    return body


y_off = W / 2 + GAP / 2
lid = lid_tray().translate((0, -y_off, 0))
base = base_tray().translate((0, y_off, 0))

result = lid.union(base)

VIEW = {"azimuth": 45, "elevation": 26}
